import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 99.4           # plate width  (X)
H = 148.0          # plate height (Z)
T = 4.2            # plate thickness (Y, features grow towards -Y)
R_CORNER = 9.8     # plate corner radius
BACK_CH = 1.8      # chamfer on back perimeter

# fork clips
CLIP_L = 10.4      # long side of clip
CLIP_S = 4.35      # short side of clip
CLIP_P = 10.9      # protrusion from plate face
SLOT_W1 = 2.4      # slot width at open (front) end
SLOT_W2 = 1.6      # slot width at closed end
SLOT_D = 8.5       # slot depth from front of clip

# flanged pins / ring bosses
FLANGE_D = 9.0
RING_D = 8.7
FLANGE_H = 2.5
PIN_AF = 4.3       # across flats of hexagonal pin
PIN_L = 13.9       # pin length from plate face
PIN_TIP_D = 3.9    # diameter of the flat pin end face (turned chamfer)
RING_HOLE_D = 3.9
FLANGE_FIL = 0.0

# small bosses / small pins
SBOSS_D = 6.4
SBOSS_H = 5.4
SBOSS_HOLE_D = 1.9
SPIN_AF = 2.6      # across flats (hexagonal)
SPIN_L = 9.2
SPIN_TIP_D = 2.2

# centre hole
BIG_HOLE_D = 12.0

# snap hook
HOOK_W = 9.7       # width at plate
HOOK_W_TIP = 7.9   # width at tip
HOOK_L = 14.7
HOOK_ZTOP = -28.8

# domes
DOME_A = 4.0       # base radius
DOME_H = 2.6       # height

# ---------------- feature layout (X right, Z up, origin = plate centre) ----------------
TOP_CLIPS = [(-18.4, 68.2), (22.0, 68.2)]                    # vertical slot
SIDE_CLIPS = [(44.0, 34.8), (43.9, -28.7), (-43.8, -30.1)]   # horizontal slot
GRID_X = (-27.0, 10.9)            # pins / ring bosses on a square grid
GRID_Z = (58.6, 20.6)
SMALL_X = (17.2, 37.0)            # small bosses / small pins
SMALL_Z = (10.2, -23.0)
BIG_HOLE_XZ = (17.5, -6.45)
DOME_XZ = [(-40.2, -64.3), (40.2, -64.3)]

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY").box(W, T, H).translate((0, T / 2.0, 0))
    .edges("|Y").fillet(R_CORNER)
    .faces(">Y").edges().chamfer(BACK_CH)
)

feats = []


def cyl(x, z, d, h, y0=0.3):
    """cylinder on plate face growing towards -Y from y0"""
    return (cq.Workplane("XZ", origin=(x, y0, z)).circle(d / 2.0)
            .extrude(h + y0))


def clip(xc, zc, vertical_slot):
    """fork clip: block with tapered slot open at the front"""
    if vertical_slot:
        sx, sz = CLIP_L, CLIP_S
    else:
        sx, sz = CLIP_S, CLIP_L
    blk = (cq.Workplane("XY").box(sx, CLIP_P + 0.3, sz)
           .translate((xc, -(CLIP_P - 0.3) / 2.0, zc)))
    yf = -CLIP_P - 1.0
    yb = -CLIP_P + SLOT_D
    pts = [(yf, -SLOT_W1 / 2.0 - 0.1), (-CLIP_P, -SLOT_W1 / 2.0),
           (yb, -SLOT_W2 / 2.0), (yb, SLOT_W2 / 2.0),
           (-CLIP_P, SLOT_W1 / 2.0), (yf, SLOT_W1 / 2.0 + 0.1)]
    if vertical_slot:
        # slot profile in XY plane (x = lateral, y = depth), cut through Z
        p2 = [(xc + b, a) for (a, b) in pts]
        cutter = (cq.Workplane("XY", origin=(0, 0, zc - sz))
                  .polyline(p2).close().extrude(2 * sz))
        endc = (cq.Workplane("XY", origin=(xc, yb, zc - sz))
                .circle(SLOT_W2 / 2.0).extrude(2 * sz))
    else:
        # slot profile in YZ plane (u = Y, v = Z), cut through X
        p2 = [(a, zc + b) for (a, b) in pts]
        cutter = (cq.Workplane("YZ", origin=(xc - sx, 0, 0))
                  .polyline(p2).close().extrude(2 * sx))
        endc = (cq.Workplane("YZ", origin=(xc - sx, yb, zc))
                .circle(SLOT_W2 / 2.0).extrude(2 * sx))
    return blk.cut(cutter).cut(endc)


def hex_pts(af):
    """hexagon with flats facing +-X, corners at +-Z (local coords of an XZ workplane)"""
    rc = af / math.sqrt(3.0)
    return [(rc * math.cos(math.pi / 6 + k * math.pi / 3),
             rc * math.sin(math.pi / 6 + k * math.pi / 3)) for k in range(6)]


def hex_pin(x, z, af, length, tip_d):
    """hexagonal pin with a turned 45 deg chamfer leaving a round end face of dia tip_d"""
    rc = af / math.sqrt(3.0)                     # corner radius of the hexagon
    prism = (cq.Workplane("XZ", origin=(x, 0.3, z)).polyline(hex_pts(af)).close()
             .extrude(length + 0.3))
    ch = rc - tip_d / 2.0 + 0.05                 # 45 deg chamfer size
    turned = (cq.Workplane("XY", origin=(x, 0, z))
              .moveTo(0, 0.3).lineTo(rc + 0.05, 0.3)
              .lineTo(rc + 0.05, -length + ch).lineTo(tip_d / 2.0, -length)
              .lineTo(0, -length).close()
              .revolve(360, (0, 0, 0), (0, 1, 0)))
    return prism.intersect(turned)


def flanged_pin(x, z):
    fl = cyl(x, z, FLANGE_D, FLANGE_H)
    if FLANGE_FIL > 0:
        fl = fl.faces("<Y").edges().fillet(FLANGE_FIL)
    pin = hex_pin(x, z, PIN_AF, PIN_L, PIN_TIP_D)
    return fl.union(pin)


def ring_boss(x, z):
    b = cyl(x, z, RING_D, FLANGE_H)
    hole = cq.Workplane("XZ", origin=(x, 0.0, z)).circle(RING_HOLE_D / 2.0).extrude(FLANGE_H + 1)
    return b.cut(hole)


def small_boss(x, z):
    b = cyl(x, z, SBOSS_D, SBOSS_H)
    hole = cq.Workplane("XZ", origin=(x, -1.5, z)).circle(SBOSS_HOLE_D / 2.0).extrude(SBOSS_H)
    return b.cut(hole)


def small_pin(x, z):
    return hex_pin(x, z, SPIN_AF, SPIN_L, SPIN_TIP_D)


def dome(x, z):
    R = (DOME_A ** 2 + DOME_H ** 2) / (2 * DOME_H)
    sph = cq.Workplane("XY").sphere(R).translate((x, R - DOME_H, z))
    keep = cq.Workplane("XY").box(2 * R + 2, DOME_H + 0.3, 2 * R + 2).translate(
        (x, -(DOME_H - 0.3) / 2.0, z))
    return sph.intersect(keep)


def hook():
    zt = HOOK_ZTOP
    pts = [
        (0.3, zt),
        (-HOOK_L, zt - 2.4),
        (-HOOK_L, zt - 4.8),
        (-HOOK_L + 4.9, zt - 7.3),
        (-HOOK_L + 4.9, zt - 4.7),
        (0.3, zt - 4.7),
    ]
    prof = (cq.Workplane("YZ", origin=(-HOOK_W, 0, 0))
            .polyline(pts).close().extrude(2 * HOOK_W))
    # drafted side walls: trapezoid in the XY plane
    trap = [(-HOOK_W / 2.0, 0.6), (HOOK_W / 2.0, 0.6),
            (HOOK_W_TIP / 2.0, -HOOK_L), (-HOOK_W_TIP / 2.0, -HOOK_L)]
    side = (cq.Workplane("XY", origin=(0, 0, zt - 10))
            .polyline(trap).close().extrude(14))
    return prof.intersect(side)


# clips
for (cx, cz) in TOP_CLIPS:
    feats.append(clip(cx, cz, True))
for (cx, cz) in SIDE_CLIPS:
    feats.append(clip(cx, cz, False))

# flanged pins and ring bosses on a square grid (diagonal pairs)
feats.append(flanged_pin(GRID_X[0], GRID_Z[0]))
feats.append(ring_boss(GRID_X[1], GRID_Z[0]))
feats.append(ring_boss(GRID_X[0], GRID_Z[1]))
feats.append(flanged_pin(GRID_X[1], GRID_Z[1]))

# small bosses / pins (diagonal pairs)
feats.append(small_boss(SMALL_X[0], SMALL_Z[0]))
feats.append(small_pin(SMALL_X[1], SMALL_Z[0]))
feats.append(small_pin(SMALL_X[0], SMALL_Z[1]))
feats.append(small_boss(SMALL_X[1], SMALL_Z[1]))

# snap hook
feats.append(hook())

# domes
for (dx, dz) in DOME_XZ:
    feats.append(dome(dx, dz))

body = plate
for f in feats:
    body = body.union(f)

# through hole in the plate
body = body.cut(
    cq.Workplane("XZ", origin=(BIG_HOLE_XZ[0], T + 1, BIG_HOLE_XZ[1]))
    .circle(BIG_HOLE_D / 2.0).extrude(T + 10)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
